import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
L = 118.2      # length along Y
H = 46.0       # height along Z
D = 34.0       # depth along X (back face at X=0, open face at X=D)
R_BACK = 6.4   # outer fillet radius around the closed back face
R_SIDE = 6.6   # outer fillet radius of the edges running front-to-back
T = 2.8        # wall thickness
RABBET = 6.0   # depth of sharp-cornered section at the opening

# central block with connector pocket
BLOCK_Y0 = -35.1             # block extent along Y (very slightly off-centre)
BLOCK_Y1 = 34.1
BLOCK_FRONT_X = 16.8          # front face of block measured from back face

RECT_HALF_Y = 22.75           # rectangular part of the hexagon pocket
POCKET_ZMIN = -5.3
POCKET_ZMAX = 16.6
TIP_HALF_Y = 31.8             # pointed ends of the hexagon pocket
TIP_DEPTH = 4.8               # depth of the flat pointed end recesses
WEB = 0.3                     # thin web between pocket and +Y pointed recess

# key notch above the pocket, open to the block front face
NOTCH_HALF_Y = 4.65
NOTCH_ZTOP = 19.9
NOTCH_DEPTH = 10.5

# figure-8 opening through the back wall (two lobes joined by a waist)
F8_Y1, F8_R1 = -5.65, 6.6    # -Y lobe centre / radius
F8_Y2, F8_R2 = 6.45, 5.95    # +Y lobe centre / radius
F8_Z = 5.9
F8_WAIST = 6.3               # height of the waist between the lobes

# round hole below the pocket
HOLE_D = 8.7
HOLE_Z = -11.4

# screw bosses near the end walls
BOSS_Y = 52.1
BOSS_R = 4.65
BOSS_FRONT_X = 28.25
BOSS_HOLE_R = 0.95
BOSS_HOLE_DEPTH = 10.0

VIEW = {"azimuth": 45, "elevation": 26}


def rounded_box(x0, x1, half_y, half_z, r_side, r_back):
    """Box from x0 to x1 with sharp edges on the x1 face; edges parallel to X
    rounded with r_side, edges around the x0 (back) face rounded with r_back."""
    b = (cq.Workplane("XY")
         .box(x1 - x0, 2 * half_y, 2 * half_z, centered=(False, True, True))
         .translate((x0, 0, 0)))
    b = b.edges("|X").fillet(r_side)
    b = b.faces("<X").edges().fillet(r_back)
    return b


# ---------------- outer shell ----------------
outer = rounded_box(0.0, D, L / 2, H / 2, R_SIDE, R_BACK)
# cavity = uniform inward offset of the outer shape, open at the front
inner_solid = rounded_box(T, D + 5.0, L / 2 - T, H / 2 - T, R_SIDE - T, R_BACK - T)
body = outer.cut(inner_solid)

# first RABBET mm behind the opening the cavity has sharp corners (lid seat)
rabbet = (cq.Workplane("XY")
          .box(RABBET + 1.0, L - 2 * T, H - 2 * T, centered=(False, True, True))
          .translate((D - RABBET, 0, 0)))
body = body.cut(rabbet)

# ---------------- central block ----------------
block = (cq.Workplane("XY")
         .box(BLOCK_FRONT_X, BLOCK_Y1 - BLOCK_Y0, H, centered=(False, False, True))
         .translate((0, BLOCK_Y0, 0)))
block = block.intersect(inner_solid)
body = body.union(block)

# ---------------- screw bosses ----------------
for sy in (-1, 1):
    boss = (cq.Workplane("YZ")
            .center(sy * BOSS_Y, 0)
            .circle(BOSS_R)
            .extrude(BOSS_FRONT_X))
    boss = boss.intersect(inner_solid)
    body = body.union(boss)
    bhole = (cq.Workplane("YZ", origin=(BOSS_FRONT_X - BOSS_HOLE_DEPTH, 0, 0))
             .center(sy * BOSS_Y, 0)
             .circle(BOSS_HOLE_R)
             .extrude(BOSS_HOLE_DEPTH + 1.0))
    body = body.cut(bhole)

# ---------------- connector pocket ----------------
pz_mid = 0.5 * (POCKET_ZMIN + POCKET_ZMAX)
# rectangular through-pocket (down to the back wall); on the +Y side it stops
# a thin web short of the pointed end recess
rect_pocket = (cq.Workplane("YZ", origin=(T, 0, 0))
               .center(-0.5 * WEB, pz_mid)
               .rect(2 * RECT_HALF_Y - WEB, POCKET_ZMAX - POCKET_ZMIN)
               .extrude(BLOCK_FRONT_X - T + 1.0))
body = body.cut(rect_pocket)

# pointed (hexagon) ends, flat bottomed
hex_pts = [
    (-TIP_HALF_Y, pz_mid),
    (-RECT_HALF_Y, POCKET_ZMIN),
    (RECT_HALF_Y, POCKET_ZMIN),
    (TIP_HALF_Y, pz_mid),
    (RECT_HALF_Y, POCKET_ZMAX),
    (-RECT_HALF_Y, POCKET_ZMAX),
]
hex_prism = (cq.Workplane("YZ", origin=(BLOCK_FRONT_X - TIP_DEPTH, 0, 0))
             .polyline(hex_pts).close()
             .extrude(TIP_DEPTH + 1.0))
# -Y end opens into the rectangular pocket
left_end = hex_prism.intersect(
    cq.Workplane("XY").box(40, TIP_HALF_Y + 1.0, 40, centered=(True, False, True))
    .translate((BLOCK_FRONT_X, -TIP_HALF_Y - 1.0, pz_mid)))
body = body.cut(left_end)
# +Y end is separated from the rectangular pocket by the thin web
right_end = hex_prism.intersect(
    cq.Workplane("XY").box(40, TIP_HALF_Y - RECT_HALF_Y + 1.0, 40,
                           centered=(True, False, True))
    .translate((BLOCK_FRONT_X, RECT_HALF_Y, pz_mid)))
body = body.cut(right_end)

# key notch above the pocket, open to the block front face
notch = (cq.Workplane("XY")
         .box(NOTCH_DEPTH + 1.0, 2 * NOTCH_HALF_Y, NOTCH_ZTOP - POCKET_ZMAX + 0.5,
              centered=(False, True, False))
         .translate((BLOCK_FRONT_X - NOTCH_DEPTH, 0, POCKET_ZMAX - 0.5)))
body = body.cut(notch)

# figure-8 opening through the back wall
fig8 = (cq.Workplane("YZ", origin=(-1.0, 0, 0))
        .pushPoints([(F8_Y1, F8_Z)]).circle(F8_R1)
        .extrude(T + 2.0))
fig8 = fig8.union(cq.Workplane("YZ", origin=(-1.0, 0, 0))
                  .pushPoints([(F8_Y2, F8_Z)]).circle(F8_R2)
                  .extrude(T + 2.0))
fig8 = fig8.union(cq.Workplane("YZ", origin=(-1.0, 0, 0))
                  .center(0.5 * (F8_Y1 + F8_Y2), F8_Z)
                  .rect(F8_Y2 - F8_Y1, F8_WAIST)
                  .extrude(T + 2.0))
body = body.cut(fig8)

# round hole through block and back wall
rh = (cq.Workplane("YZ", origin=(-1.0, 0, 0))
      .center(0, HOLE_Z)
      .circle(HOLE_D / 2)
      .extrude(BLOCK_FRONT_X + 2.0))
body = body.cut(rh)

result = body
